import math
import cadquery as cq

# ---------------------------------------------------------------
# Smart-servo style actuator (frame with nut-trap tabs, horn, idler)
# X : horn axis (horn on +X), Y : long axis, Z : up
# ---------------------------------------------------------------

# overall
Y0 = -23.25          # -Y end of the frame rails / corner columns
Y1 = 23.25           # +Y end of the rounded housing
XF = 14.5            # half width of frame (X)
XR = 9.9             # inner x of the side rails
ZB = 11.85           # half height of body
ZT = 14.6            # top of the tabs
YR_END = 10.3        # rails end here, rounded housing beyond

# -Y face of the core body
YBF_TOP = -20.78     # top band face (set back)
YBF_LOW = -21.88     # middle / lower band face
Z_LEDGE = 5.4
Z_GROOVE = -5.0
EDGE_A = 0.6         # -Y top edge rounding (Y extent)
EDGE_B = 0.7         # -Y top edge rounding (Z extent)
EDGE_BOT_A = 1.6     # -Y bottom edge rounding (Y extent)
EDGE_BOT_B = 1.8     # -Y bottom edge rounding (Z extent)

# housing (+Y end)
Y_HOUSE0 = 9.0
R_END = 4.4          # rounding of +Y end (in YZ)
R_LONG = 2.6         # rounding of the long edges of the housing

# tabs
TAB_YC = [-15.9, -8.55, -1.2, 6.15]
TAB_W = 6.0
Z_NOTCH = 13.3       # floor of notches between tabs
RAMP = 1.85          # outer ramp (chamfer) on the notch floors
HOLE_Z = 12.2
HOLE_D = 2.2
POCKET_X = 12.7      # pockets span XR..POCKET_X
POCKET_W = 4.0
POCKET_BOT = 2.4     # width of tapered pocket floor
POCKET_Z0 = 11.65    # pocket floor height
POCKET_ZS = 12.6     # taper starts here
TAB_CH = 1.0

# -Y corner columns
Z_STEP1 = 10.3
Z_STEP2 = 11.35
Y_STEP = -21.9
Y_STEP2 = -20.1
COL_CH = 1.0         # chamfer on the outer vertical edge of the corner column
MID_CH = 1.9         # chamfer of the cut-back middle part of the column
Z_MIDCUT = 4.2
NUT_Y = -21.0
NUT_Z = 7.4
NUT_ZH = 3.5

# +X side cover panel
PANEL_T = 2.6
PANEL_Y = (-17.9, 4.6)
PANEL_Z = 9.1
PAD_Y = (4.6, 18.3)    # thin pad under the horn
PAD_T = 0.8
LABEL_Y = (-11.5, -3.0)
LABEL_Z = 7.2

# horn
HORN_Y = 12.5
HORN_R = 10.0
HORN_X0 = XF + 0.8
HORN_T = 3.7
HORN_BASE_R = 8.5
HORN_BIG_R = 7.2
HORN_BIG_D = 2.0
HORN_SMALL_R = 4.8
HORN_SMALL_D = 1.2

# idler boss (-X)
BOSS_R = 5.1
BOSS_H = 2.9

# rectangular bosses (-X)
RB_Y = (-18.1, -11.3)
RB_Z = (4.0, 9.1)
RB_H = 2.4

# connector opening (-X)
CON_Y = (-5.4, 1.0)
CON_Z = 9.0
CON_SLOT = 1.6

# screws on +X
SCREWS_FRONT = [(-18.5, 9.7), (-18.5, -9.7)]
SCREWS_BACK = [(20.0, 8.85), (20.0, -8.85)]
CORNER_REC_Y = 18.3    # screw recesses at the +X/+Y corners
CORNER_REC_X = 12.85
CORNER_REC_Z = 7.2
END_CUT_X = 10.7      # middle of the +X/+Y corner is cut back to here
END_CUT_Z = 7.0
SCREW_R = 1.45


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(abs(x1 - x0), abs(y1 - y0), abs(z1 - z0))
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def cyl_x(x0, x1, y, z, r):
    return (cq.Workplane("YZ", origin=(min(x0, x1), 0, 0))
            .center(y, z).circle(r).extrude(abs(x1 - x0)))


def cyl_y(y0, y1, x, z, r):
    return (cq.Workplane("XZ", origin=(0, max(y0, y1), 0))
            .center(x, z).circle(r).extrude(abs(y1 - y0)))


def cyl_z(z0, z1, x, y, r):
    return (cq.Workplane("XY", origin=(0, 0, min(z0, z1)))
            .center(x, y).circle(r).extrude(abs(z1 - z0)))


# ---------------- core body (between rails) ----------------
core_prof = (cq.Workplane("YZ", origin=(-XR, 0, 0))
             .moveTo(YR_END + 1.0, -ZB)
             .lineTo(YR_END + 1.0, ZB)
             .lineTo(YBF_TOP + EDGE_A, ZB)
             .spline([(YBF_TOP, ZB - EDGE_B)], tangents=[(-1, 0), (0, -1)],
                     includeCurrent=True)
             .lineTo(YBF_TOP, Z_LEDGE)
             .lineTo(YBF_LOW, Z_LEDGE)
             .lineTo(YBF_LOW, -ZB + EDGE_BOT_B)
             .spline([(YBF_LOW + EDGE_BOT_A, -ZB)], tangents=[(0, -1), (1, 0)],
                     includeCurrent=True)
             .close())
core = core_prof.extrude(2 * XR)

# groove on the -Y face
core = core.cut(box(-XR - 1, XR + 1, YBF_LOW - 1, YBF_LOW + 0.3,
                    Z_GROOVE - 0.2, Z_GROOVE + 0.2))

# ---------------- housing (+Y end, rounded) ----------------
housing = box(-XF, XF, Y_HOUSE0, Y1, -ZB, ZB)
housing = housing.edges("|X and >Y").fillet(R_END)
housing = housing.edges("|Y").fillet(R_LONG)

body = core.union(housing)

# ---------------- side rails with tabs ----------------
# top edge of the rail profile as (y_start, y_end, z_top) segments
segs = [(Y0, Y_STEP, Z_STEP1), (Y_STEP, Y_STEP2, Z_STEP2),
        (Y_STEP2, TAB_YC[0] - TAB_W / 2, Z_NOTCH)]
prev = TAB_YC[0] - TAB_W / 2
for yc in TAB_YC:
    a, b = yc - TAB_W / 2, yc + TAB_W / 2
    if a > prev + 1e-6:
        segs.append((prev, a, Z_NOTCH))
    segs.append((a, b, ZT))
    prev = b
segs.append((prev, YR_END, Z_NOTCH))
notch_segs = [(a, b) for (a, b, z) in segs if abs(z - Z_NOTCH) < 1e-6]

pts = []
for (a, b, z) in segs:                 # top edge, -Y to +Y
    pts += [(a, z), (b, z)]
for (a, b, z) in reversed(segs):       # bottom edge (mirror), +Y to -Y
    pts += [(b, -z), (a, -z)]
pts += [(Y0, -Z_MIDCUT), (Y_STEP, -Z_MIDCUT), (Y_STEP, Z_MIDCUT), (Y0, Z_MIDCUT)]

clean = []
for p in pts:
    if not clean or abs(clean[-1][0] - p[0]) > 1e-6 or abs(clean[-1][1] - p[1]) > 1e-6:
        clean.append(p)
if abs(clean[0][0] - clean[-1][0]) < 1e-6 and abs(clean[0][1] - clean[-1][1]) < 1e-6:
    clean.pop()


def rail(side):
    x0 = XR if side > 0 else -XF
    xo = side * XF
    r = (cq.Workplane("YZ", origin=(x0, 0, 0))
         .polyline(clean).close().extrude(XF - XR))
    # chamfer the outer top / bottom edges of every step and tab
    sel = cq.selectors.BoxSelector((xo - 0.01, Y0 - 0.01, -ZT - 0.01),
                                   (xo + 0.01, YR_END - 0.5, ZT + 0.01))
    edges = [e for e in r.edges("|Y").edges(sel).vals()
             if abs(e.Center().z) > Z_MIDCUT + 0.5
             and abs(abs(e.Center().z) - Z_NOTCH) > 0.05]
    r = r.newObject(edges).chamfer(TAB_CH)
    # sloped (ramped) outer edge of the notch floors
    for t in (1, -1):
        for (a, b) in notch_segs:
            ramp = (cq.Workplane("XZ", origin=(0, b + 0.01, 0))
                    .polyline([(xo - side * RAMP, t * Z_NOTCH), (xo + side * 1, t * (Z_NOTCH + 1 + RAMP)),
                               (xo + side * 1, t * (Z_NOTCH - RAMP - 1)), (xo, t * (Z_NOTCH - RAMP))])
                    .close().extrude(b - a + 0.02))
            r = r.cut(ramp)
    # chamfer of the vertical outer edge of the -Y corner column
    for t in (1, -1):
        za, zb = sorted((t * (Z_MIDCUT - 0.01), t * (ZT + 1)))
        tri = (cq.Workplane("XY", origin=(0, 0, za))
               .polyline([(xo - side * COL_CH, Y0 - 1), (xo + side * 1, Y0 - 1),
                          (xo + side * 1, Y0 + COL_CH + 1), (xo, Y0 + COL_CH),
                          (xo - side * COL_CH, Y0)]).close()
               .extrude(zb - za))
        r = r.cut(tri)
    tri = (cq.Workplane("XY", origin=(0, 0, -Z_MIDCUT))
           .polyline([(xo - side * MID_CH, Y_STEP - 1), (xo + side * 1, Y_STEP - 1),
                      (xo + side * 1, Y_STEP + MID_CH + 1), (xo, Y_STEP + MID_CH),
                      (xo - side * MID_CH, Y_STEP)]).close()
           .extrude(2 * Z_MIDCUT))
    r = r.cut(tri)
    # nut pockets + bolt holes in tabs
    xc = side * (XR + POCKET_X) / 2
    pr = (POCKET_X - XR) / 2
    for t in (1, -1):
        for yc in TAB_YC:
            hw = POCKET_W / 2
            prof = [(yc - POCKET_BOT / 2, t * POCKET_Z0), (yc + POCKET_BOT / 2, t * POCKET_Z0),
                    (yc + hw, t * POCKET_ZS), (yc + hw, t * (ZT + 1)),
                    (yc - hw, t * (ZT + 1)), (yc - hw, t * POCKET_ZS)]
            xa, xb = sorted((side * (XR - 0.05), side * POCKET_X))
            pk = (cq.Workplane("YZ", origin=(xa, 0, 0)).polyline(prof).close()
                  .extrude(xb - xa))
            # curved floor rising towards the outer wall
            rr = POCKET_X - XR
            zc = t * (POCKET_Z0 + rr)
            za, zb = sorted((zc, t * (ZT + 1)))
            shape = (cyl_y(yc - hw - 1, yc + hw + 1, side * XR, zc, rr)
                     .union(box(xa - 1, xb + 1, yc - hw - 1, yc + hw + 1, za, zb)))
            r = r.cut(pk.intersect(shape))
            r = r.cut(cyl_x(side * 11.5, side * (XF + 1), yc, t * HOLE_Z, HOLE_D / 2))
        # nut slots on the -Y face of the corner column
        xa, xb = sorted((side * XR, side * POCKET_X))
        za, zb = sorted((t * (NUT_Z - NUT_ZH / 2), t * (NUT_Z + NUT_ZH / 2)))
        r = r.cut(box(xa, xb, Y0 - 1, NUT_Y, za, zb))
        r = r.cut(cyl_z(za, zb, xc, NUT_Y, pr))
        r = r.cut(cyl_x(side * 11.5, side * (XF + 1), NUT_Y, t * NUT_Z, HOLE_D / 2))
    return r


body = body.union(rail(1)).union(rail(-1))

# ---------------- +X cover panel ----------------
panel = (cq.Workplane("YZ", origin=(XF - 0.2, 0, 0))
         .center((PANEL_Y[0] + PANEL_Y[1]) / 2, 0)
         .rect(PANEL_Y[1] - PANEL_Y[0], 2 * PANEL_Z)
         .extrude(PANEL_T + 0.2))
panel = panel.edges("|X").fillet(1.0)
panel = panel.faces(">X").edges().fillet(1.0)
panel = panel.cut(cyl_x(XF - 1, XF + PANEL_T + 1, HORN_Y, 0, HORN_R + 0.4))
for (sy, sz) in SCREWS_FRONT:
    panel = panel.cut(cyl_x(XF - 1, XF + PANEL_T + 1, sy, sz, SCREW_R + 0.45))
# label recess
panel = panel.cut(box(XF + PANEL_T - 0.15, XF + PANEL_T + 1,
                      LABEL_Y[0], LABEL_Y[1], -LABEL_Z, LABEL_Z))
body = body.union(panel)
pad = (cq.Workplane("YZ", origin=(XF - 0.2, 0, 0))
       .center((PAD_Y[0] + PAD_Y[1]) / 2, 0)
       .rect(PAD_Y[1] - PAD_Y[0], 2 * PANEL_Z)
       .extrude(PAD_T + 0.2))
pad = pad.edges("|X").fillet(0.8)
body = body.union(pad)

# ---------------- horn ----------------
horn_base = cyl_x(XF + PAD_T - 0.1, HORN_X0 + 0.01, HORN_Y, 0, HORN_BASE_R)
horn = cyl_x(HORN_X0, HORN_X0 + HORN_T, HORN_Y, 0, HORN_R)
horn = horn.faces(">X").edges().chamfer(0.25)
hx1 = HORN_X0 + HORN_T
for k in range(4):
    a = math.radians(90 * k)
    hy, hz = HORN_Y + HORN_BIG_R * math.cos(a), HORN_BIG_R * math.sin(a)
    horn = horn.cut(cyl_x(hx1 - 3.0, hx1 + 1, hy, hz, HORN_BIG_D / 2))
    horn = horn.cut(cyl_x(hx1 - 0.25, hx1 + 1, hy, hz, HORN_BIG_D / 2 + 0.3))
for ang in (60, 180, 300):
    a = math.radians(ang)
    horn = horn.cut(cyl_x(hx1 - 2.0, hx1 + 1, HORN_Y + HORN_SMALL_R * math.cos(a),
                          HORN_SMALL_R * math.sin(a), HORN_SMALL_D / 2))
# slit from +Y hole to rim and marker notch on -Y rim
horn = horn.cut(box(HORN_X0 - 1, hx1 + 1, HORN_Y + HORN_BIG_R, HORN_Y + HORN_R + 1,
                    -0.15, 0.15))
horn = horn.cut(box(HORN_X0 - 1, hx1 + 1, HORN_Y - HORN_R - 1, HORN_Y - HORN_R + 0.35,
                    -0.45, 0.45))
# centre counterbore + screw
horn = horn.cut(cyl_x(hx1 - 1.0, hx1 + 1, HORN_Y, 0, 2.9))
screw = cyl_x(hx1 - 1.01, hx1 - 0.2, HORN_Y, 0, 2.4)
screw = screw.faces(">X").edges().fillet(0.5)
screw = screw.cut(box(hx1 - 0.8, hx1 + 1, HORN_Y - 1.6, HORN_Y + 1.6, -0.3, 0.3))
screw = screw.cut(box(hx1 - 0.8, hx1 + 1, HORN_Y - 0.3, HORN_Y + 0.3, -1.6, 1.6))
horn = horn.union(screw).union(horn_base)
body = body.union(horn)

# ---------------- screws on +X face ----------------
def pan_screw(x_base, y, z, r=SCREW_R, h=0.7):
    s = cyl_x(x_base - 0.05, x_base + h, y, z, r)
    s = s.faces(">X").edges().fillet(0.35)
    s = s.cut(box(x_base + h - 0.35, x_base + h + 1, y - r * 0.7, y + r * 0.7, z - 0.17, z + 0.17))
    s = s.cut(box(x_base + h - 0.35, x_base + h + 1, y - 0.17, y + 0.17, z - r * 0.7, z + r * 0.7))
    return s


for (sy, sz) in SCREWS_FRONT:
    body = body.cut(cyl_x(XF - 0.6, XF + 1, sy, sz, SCREW_R + 0.3))
    body = body.union(pan_screw(XF - 0.6, sy, sz))
for t in (1, -1):
    za, zb = sorted((t * CORNER_REC_Z, t * (ZB + 1)))
    body = body.cut(box(CORNER_REC_X, XF + 1, CORNER_REC_Y, Y1 + 1, za, zb))
body = body.cut(box(END_CUT_X, XF + 1, CORNER_REC_Y, Y1 + 1, -END_CUT_Z, END_CUT_Z))
# the horn hub continues into this opening (coaxial drum, visible from behind)
drum = box(END_CUT_X - 0.1, HORN_X0 + 0.05, CORNER_REC_Y - 0.1, Y1, -END_CUT_Z, END_CUT_Z).intersect(
    cyl_x(END_CUT_X - 0.1, HORN_X0 + 0.05, HORN_Y, 0, HORN_R))
drum = drum.cut(box(END_CUT_X - 1, HORN_X0 + 1, HORN_Y + HORN_R - 0.6, HORN_Y + HORN_R + 1,
                    -0.15, 0.15))
body = body.union(drum)
for (sy, sz) in SCREWS_BACK:
    body = body.union(pan_screw(CORNER_REC_X, sy, sz))

# ---------------- -X side features ----------------
boss = cyl_x(-XF - BOSS_H, -XF + 0.5, HORN_Y, 0, BOSS_R)
boss = boss.faces("<X").edges().chamfer(0.6)
boss = boss.cut(cyl_x(-XF - BOSS_H - 1, -XF - BOSS_H + 0.4, HORN_Y, 0, 3.0))
boss = boss.cut(cyl_x(-XF - BOSS_H - 1, -XF - BOSS_H + 2.4, HORN_Y, 0, 1.1))
body = body.union(boss)

for t in (1, -1):
    za, zb = sorted((t * RB_Z[0], t * RB_Z[1]))
    rb = box(-XF - RB_H, -XF + 0.3, RB_Y[0], RB_Y[1], za, zb)
    rb = rb.faces("<X").edges().fillet(0.4)
    body = body.union(rb)

# connector opening with two ports
body = body.cut(box(-XF - 1, -XF + 0.8, CON_Y[0], CON_Y[1], -CON_Z, CON_Z))
for t in (1, -1):
    za, zb = sorted((t * 0.7, t * (CON_Z - 0.6)))
    # shallow port mouth, deep pin slot on its +Y side
    body = body.cut(box(-XF - 1, -XF + 2.0, CON_Y[0] + 0.6, CON_Y[1] - 0.6, za, zb))
    body = body.cut(box(-XF - 1, -XF + 5.0, CON_Y[1] - 0.6 - CON_SLOT, CON_Y[1] - 0.6, za, zb))
    # row of contact pins in the slot
    zs = sorted((t * 1.6, t * (CON_Z - 1.5)))
    npin = 4
    for k in range(npin):
        zp = zs[0] + (zs[1] - zs[0]) * k / (npin - 1)
        body = body.union(box(-XF + 1.6, -XF + 5.05, CON_Y[1] - 0.6 - 0.55, CON_Y[1] - 0.6 - 0.15,
                              zp - 0.2, zp + 0.2))

# small holes on -X face
for (hy, hz) in [(19.6, 5.5), (19.6, -5.5), (6.6, 7.0), (6.6, -7.0),
                 (-8.3, 7.3), (-8.3, -7.3)]:
    body = body.cut(cyl_x(-XF - 1, -XF + 2.0, hy, hz, 0.6))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
